import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 38.0            # outer (land) diameter of the grip
H = 23.75           # overall height
TOP_CH = 2.15       # 45 deg chamfer on the top outer edge
BOT_CH = 1.0        # 45 deg chamfer on the bottom outer edge

N_GROOVES = 20      # number of flutes around the grip
GROOVE_R = 3.25     # radius of each concave flute
GROOVE_DEPTH = 0.55 # radial depth of the flute into the land

BORE_D = 22.0       # main blind bore from the underside
BORE_DEPTH = 12.0
BORE_CH = 0.8       # 45 deg chamfer at the bore mouth
CONE_D = 14.5       # conical recess in the bore ceiling (mouth diameter)
CONE_ANGLE = 90.0   # included angle of the conical recess

# angular position of the (invisible) revolve seams, kept out of the main views
OUTER_SEAM_DEG = 135.0
BORE_SEAM_DEG = -45.0

R = D / 2.0
cone_h = (CONE_D / 2.0) / math.tan(math.radians(CONE_ANGLE / 2.0))


def revolve_profile(pts, seam_deg):
    """Revolve an (r, z) polygon 360 deg about the global Z axis."""
    return (
        cq.Workplane("XZ")
        .polyline(pts)
        .close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), seam_deg)
    )


# ---------------- outer body: cylinder with top and bottom chamfers ----------------
outer = revolve_profile(
    [
        (0.0, 0.0),
        (R - BOT_CH, 0.0),
        (R, BOT_CH),
        (R, H - TOP_CH),
        (R - TOP_CH, H),
        (0.0, H),
    ],
    OUTER_SEAM_DEG,
)

# ---------------- underside bore: chamfered mouth, flat shoulder, conical recess ----------------
ext = 1.0  # cutter runs out below the bottom face
bore = revolve_profile(
    [
        (0.0, -ext),
        (BORE_D / 2.0 + BORE_CH + ext, -ext),
        (BORE_D / 2.0, BORE_CH),
        (BORE_D / 2.0, BORE_DEPTH),
        (CONE_D / 2.0, BORE_DEPTH),
        (0.0, BORE_DEPTH + cone_h),
    ],
    BORE_SEAM_DEG,
)

body = outer.cut(bore)

# ---------------- flutes: polar pattern of cylindrical cutters ----------------
# Adjacent cutters overlap each other (outside the part), so the pattern is cut
# in two interleaved batches of non-overlapping circles.
gc = R + GROOVE_R - GROOVE_DEPTH   # radius of the circle carrying the flute axes


def flute_batch(start):
    pts = []
    for i in range(start, N_GROOVES, 2):
        a = math.radians(360.0 / N_GROOVES * i)
        pts.append((gc * math.cos(a), gc * math.sin(a)))
    return (
        cq.Workplane("XY")
        .workplane(offset=-1.0)
        .pushPoints(pts)
        .circle(GROOVE_R)
        .extrude(H + 2.0)
    )


result = body.cut(flute_batch(0)).cut(flute_batch(1))

VIEW = {"azimuth": 45, "elevation": 26}
